import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
L = 76.0          # length along X
W = 56.0          # width along Y
H = 60.0          # height (bottom to top plateau)

BASE_H = 12.6     # height of the bottom plate
GROOVE_H = 2.2    # height of the parting groove
GROOVE_D = 0.8    # depth of the parting groove
EDGE_C = 0.6      # vertical edge chamfer
BASE_TOP_C = 0.3  # chamfer on the top outer edge of the base

LEDGE_W = 2.0     # width of the raised rim along the +/-Y top edges
LEDGE_D = 0.15    # height of that rim above the plateau
TOP_Y_C = 0.4     # chamfer of the +/-Y top edges
TOP_X_R = 0.6     # rounding of the +/-X top edges
LEDGE_O = 0.8     # rim width around the corner pockets
LEDGE_RND = 4.0   # rounding where the rim turns around a pocket

CP_A = 8.6        # corner pocket size (square)
CP_R = 4.2        # corner pocket inner radius
CP_DEPTH = 4.8    # corner pocket depth
CP_HOLE = 4.5     # through hole in corner pocket
CP_HOLE_OFF = 4.1 # hole centre distance from the outer faces

BOT_DEPTH = 0.35  # depth of the corner spot faces on the underside
BLIND_DEPTH = 10.0
BLIND_HOLE = 4.2
BOT_CB_D = 5.6     # counterbore at the underside of the corner holes
BOT_CB_DEPTH = 0.8

# jaw-mount pads (two, 180 deg rotated)
PAD_CX = 18.2
PAD_CY = 16.0
PAD_POCKET_L = 37.2
PAD_POCKET_W = 11.6
PAD_POCKET_D = 1.0
PAD_SLOT_D = 4.5      # depth of the open slot beyond the jaw's outer end
PAD_L = 22.7
PAD_W = 11.1
PAD_PROUD = 1.3       # pad top above plateau
PAD_HOLE = 4.4
PAD_HOLE_DX = 7.2
PAD_PIN = 2.0
PAD_PIN_DX = 9.6
PAD_PIN_DY = 3.5
PAD_NOTCH_R = 3.1
PAD_NOTCH_DX = 1.9
PAD_HOLE_DEPTH = 6.0

# side cover plates (on +X and -X faces, 180 deg rotated)
PANEL_Y0 = -18.5
PANEL_Y1 = 26.0
PANEL_ZB = 35.4
PANEL_R = 4.4
PANEL_T = 0.3
SCREW_D = 4.2
SCREW_T = 0.6
SCREW_INSET = 4.3

# connector on -X face
CON_Z = 14.0
CON_NECK_D = 8.5
CON_NECK_L = 1.5
CON_NUT_D = 10.8
CON_NUT_L = 3.4
CON_MID_D = 8.5
CON_MID_L = 1.9
CON_CAP_D = 9.2
CON_CAP_L = 2.7

# engraved logo ring on the back face
LOGO_D = 14.0
LOGO_W = 0.6
LOGO_DEPTH = 0.3
LOGO_Z = 30.0

# oblong recess on the back face of the base
SLOT_L = 11.0
SLOT_H = 4.5
SLOT_D = 0.5
SLOT_Z = 6.3

hx, hy = L / 2.0, W / 2.0


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def corner_pocket_profile(wp, sx, sy, a, r, ext=1.5):
    """Closed 2D profile of an L-open corner pocket whose wall is one smooth
    curve (straight - quarter round - straight).  sx, sy = +/-1 pick the
    body corner."""
    cx, cy = sx * hx, sy * hy

    def g(u, v):
        # local u, v point outward; body is u<0, v<0
        return (cx + sx * u, cy + sy * v)

    c = (-a + r, -a + r)
    s22, c22 = math.sin(math.radians(22.5)), math.cos(math.radians(22.5))
    k = 1.0 / math.sqrt(2.0)
    loc = [(-a, (ext - a + r) / 2.0), (-a, -a + r),
           (c[0] - r * c22, c[1] - r * s22),
           (c[0] - r * k, c[1] - r * k),
           (c[0] - r * s22, c[1] - r * c22),
           (-a + r, -a), ((ext - a + r) / 2.0, -a), (ext, -a)]
    t0 = (0.0, -1.0 * sy)
    t1 = (1.0 * sx, 0.0)
    w = wp.moveTo(*g(ext, ext)).lineTo(*g(-a, ext))
    w = w.spline([g(*p) for p in loc], tangents=[t0, t1], includeCurrent=True)
    return w.close()


def corner_pocket(sx, sy, a, r, z0, z1):
    wp = cq.Workplane("XY").workplane(offset=z0)
    return corner_pocket_profile(wp, sx, sy, a, r).extrude(z1 - z0)


def plateau_outline(xe=0.0):
    """Outline of the slightly sunk top plateau: everything except the narrow
    raised rim along the +/-Y edges and around the two corner pockets
    (180 deg symmetric).  xe extends the outline past the +/-X faces."""
    yl = hy - LEDGE_W
    rc = CP_R + LEDGE_O
    # (-X,+Y) pocket rounded-corner centre
    ccx, ccy = -hx + CP_A - CP_R, hy - CP_A + CP_R
    rr = LEDGE_RND
    # convex arc centre P=(px, yl-rr), externally tangent to circle (C, rc)
    dy = yl - rr - ccy
    px = ccx + math.sqrt((rc + rr) ** 2 - dy ** 2)
    py = yl - rr
    dist = math.hypot(px - ccx, py - ccy)
    tx = ccx + rc * (px - ccx) / dist
    ty = ccy + rc * (py - ccy) / dist
    # convex arc from angle 90 deg to angle of T about P
    a0 = math.pi / 2.0
    a1 = math.atan2(ty - py, tx - px)
    am = 0.5 * (a0 + a1)
    m1 = (px + rr * math.cos(am), py + rr * math.sin(am))
    # concave arc about C from angle of T to -90 deg
    b0 = math.atan2(ty - ccy, tx - ccx)
    b1 = -math.pi / 2.0
    bm = 0.5 * (b0 + b1)
    m2 = (ccx + rc * math.cos(bm), ccy + rc * math.sin(bm))
    q1 = (px, yl)
    t = (tx, ty)
    q3 = (ccx, ccy - rc)

    def n(p):
        return (-p[0], -p[1])

    w = cq.Workplane("XY").moveTo(-hx - xe, -yl)
    w = w.lineTo(*n(q1)).threePointArc(n(m1), n(t)).threePointArc(n(m2), n(q3))
    w = w.lineTo(hx + xe, -q3[1]).lineTo(hx + xe, yl)
    w = w.lineTo(*q1).threePointArc(m1, t).threePointArc(m2, q3)
    w = w.lineTo(-hx - xe, q3[1]).close()
    return w


# ---------------------------------------------------------------------------
# main body
# ---------------------------------------------------------------------------
base = (cq.Workplane("XY").box(L, W, BASE_H, centered=(True, True, False))
        .edges("|Z").chamfer(EDGE_C)
        .faces(">Z").edges().chamfer(BASE_TOP_C))
groove = (cq.Workplane("XY").workplane(offset=BASE_H - 0.1)
          .box(L - 2 * GROOVE_D, W - 2 * GROOVE_D, GROOVE_H + 0.2,
               centered=(True, True, False))
          .edges("|Z").chamfer(EDGE_C))
upper_z0 = BASE_H + GROOVE_H
upper = (cq.Workplane("XY").workplane(offset=upper_z0)
         .box(L, W, H - upper_z0, centered=(True, True, False))
         .edges("|Z").chamfer(EDGE_C)
         .faces(">Z").edges("|X").chamfer(TOP_Y_C)
         .faces(">Z").edges("|Y").fillet(TOP_X_R))
# sink the plateau slightly, leaving the narrow rim standing
plateau_cut = (plateau_outline(1.0).extrude(LEDGE_D + 1.0)
               .translate((0, 0, H - LEDGE_D)))

body = base.union(groove).union(upper).cut(plateau_cut)

# ---------------------------------------------------------------------------
# corner pockets (top) with through holes, spot faces (bottom)
# ---------------------------------------------------------------------------
for sx, sy in ((1, -1), (-1, 1)):
    body = body.cut(corner_pocket(sx, sy, CP_A, CP_R, H - CP_DEPTH, H + 5.0))

for sx, sy in ((1, -1), (-1, 1), (1, 1), (-1, -1)):
    sp = corner_pocket(sx, sy, CP_A, CP_R, -5.0, BOT_DEPTH)
    body = body.cut(sp)

for sx, sy in ((1, -1), (-1, 1)):
    hc = (sx * (hx - CP_HOLE_OFF), sy * (hy - CP_HOLE_OFF))
    hole = (cq.Workplane("XY").center(*hc).circle(CP_HOLE / 2.0)
            .extrude(H + 2).translate((0, 0, -1)))
    body = body.cut(hole)
for sx, sy in ((1, 1), (-1, -1)):
    hc = (sx * (hx - CP_HOLE_OFF), sy * (hy - CP_HOLE_OFF))
    hole = (cq.Workplane("XY").center(*hc).circle(BLIND_HOLE / 2.0)
            .extrude(BLIND_DEPTH + 1).translate((0, 0, -1)))
    body = body.cut(hole)
# small counterbores at the underside of all four corner holes
cbores = (cq.Workplane("XY").workplane(offset=-1.0)
          .pushPoints([(sx * (hx - CP_HOLE_OFF), sy * (hy - CP_HOLE_OFF))
                       for sx in (-1, 1) for sy in (-1, 1)])
          .circle(BOT_CB_D / 2.0).extrude(1.0 + BOT_DEPTH + BOT_CB_DEPTH))
body = body.cut(cbores)

# ---------------------------------------------------------------------------
# jaw-mount pads
# ---------------------------------------------------------------------------
def pad(sign):
    """sign=-1 : pad at (-X,-Y); sign=+1 : pad at (+X,+Y) (180 deg copy)."""
    cx, cy = sign * PAD_CX, sign * PAD_CY
    floor_z = H - PAD_POCKET_D
    pocket = (cq.Workplane("XY").workplane(offset=floor_z)
              .center(cx, cy).rect(PAD_POCKET_L, PAD_POCKET_W).extrude(5.0))
    # deep jaw-travel slot between the jaw's outer end and the pocket end
    x_in = cx + sign * PAD_L / 2.0
    x_out = cx + sign * PAD_POCKET_L / 2.0
    slot_len = abs(x_out - x_in)
    deep = (cq.Workplane("XY").workplane(offset=H - PAD_SLOT_D)
            .center((x_in + x_out) / 2.0, cy)
            .rect(slot_len, PAD_POCKET_W).extrude(PAD_SLOT_D + 5.0))
    pocket = pocket.union(deep)
    block = (cq.Workplane("XY").workplane(offset=floor_z - 0.01)
             .center(cx, cy).rect(PAD_L, PAD_W)
             .extrude(PAD_POCKET_D + PAD_PROUD + 0.01))
    # side notches
    nx = cx - sign * PAD_NOTCH_DX
    notches = (cq.Workplane("XY").workplane(offset=floor_z - 1)
               .pushPoints([(nx, cy + PAD_W / 2.0), (nx, cy - PAD_W / 2.0)])
               .circle(PAD_NOTCH_R).extrude(10))
    block = block.cut(notches)
    holes = (cq.Workplane("XY").workplane(offset=H + PAD_PROUD - PAD_HOLE_DEPTH)
             .pushPoints([(cx - PAD_HOLE_DX, cy), (cx + PAD_HOLE_DX, cy)])
             .circle(PAD_HOLE / 2.0).extrude(PAD_HOLE_DEPTH + 1))
    pins = (cq.Workplane("XY").workplane(offset=H + PAD_PROUD - 4.0)
            .pushPoints([(cx + sign * PAD_PIN_DX, cy + sign * PAD_PIN_DY),
                         (cx - sign * PAD_PIN_DX, cy - sign * PAD_PIN_DY)])
            .circle(PAD_PIN / 2.0).extrude(5.0))
    return pocket, block, holes.union(pins)


for s in (-1, 1):
    pk, bl, hl = pad(s)
    body = body.cut(pk).union(bl).cut(hl)

# ---------------------------------------------------------------------------
# side cover plates with screw heads (+X face and rotated copy on -X face)
# ---------------------------------------------------------------------------
def side_panel():
    pw = PANEL_Y1 - PANEL_Y0
    ph = H - PANEL_ZB
    yc = (PANEL_Y0 + PANEL_Y1) / 2.0
    plate = (cq.Workplane("YZ").workplane(offset=hx - 0.01)
             .center(yc, PANEL_ZB + ph / 2.0).rect(pw, ph)
             .extrude(PANEL_T + 0.01))
    plate = plate.edges("|X").edges("<Z").fillet(PANEL_R)
    screws = (cq.Workplane("YZ").workplane(offset=hx + PANEL_T - 0.01)
              .pushPoints([(PANEL_Y0 + SCREW_INSET, PANEL_ZB + SCREW_INSET),
                           (PANEL_Y1 - SCREW_INSET, PANEL_ZB + SCREW_INSET)])
              .circle(SCREW_D / 2.0).extrude(SCREW_T + 0.01))
    return plate.union(screws)


sp_right = side_panel()
sp_left = side_panel().rotate((0, 0, 0), (0, 0, 1), 180)
body = body.union(sp_right).union(sp_left)

# ---------------------------------------------------------------------------
# round connector on the -X face
# ---------------------------------------------------------------------------
def cyl(d, x0, length):
    return (cq.Workplane("YZ").workplane(offset=x0).center(0, CON_Z)
            .circle(d / 2.0).extrude(length))


neck = cyl(CON_NECK_D, -hx - CON_NECK_L, CON_NECK_L + GROOVE_D + 0.2)
nut = cyl(CON_NUT_D, -hx - CON_NECK_L - CON_NUT_L, CON_NUT_L)
mid = cyl(CON_MID_D, -hx - CON_NECK_L - CON_NUT_L - CON_MID_L, CON_MID_L)
xcap = -hx - CON_NECK_L - CON_NUT_L - CON_MID_L - CON_CAP_L
cap = cyl(CON_CAP_D, xcap, CON_CAP_L)
cap = cap.faces("<X").edges().fillet(0.6)
nut = nut.edges().chamfer(0.4)
conn = neck.union(nut).union(mid).union(cap)
# pin insert recess in the end face
recess = cyl(7.8, xcap - 1, 2.0)
insert = cyl(7.0, xcap + 0.4, 1.0)
conn = conn.cut(recess).union(insert)
body = body.union(conn)

# ---------------------------------------------------------------------------
# oblong recess on the back (+Y) face of the base
# ---------------------------------------------------------------------------
slot = (cq.Workplane("XZ").workplane(offset=-hy - 1)
        .center(0, SLOT_Z).slot2D(SLOT_L, SLOT_H).extrude(1 + SLOT_D))
body = body.cut(slot)

# ---------------------------------------------------------------------------
# engraved logo ring on the back (+Y) face of the housing
# ---------------------------------------------------------------------------
ring = (cq.Workplane("XZ").workplane(offset=-hy - 1)
        .center(0, LOGO_Z).circle(LOGO_D / 2.0).circle(LOGO_D / 2.0 - LOGO_W)
        .extrude(1 + LOGO_DEPTH))
body = body.cut(ring)

result = body
